import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Reducing socket / spigot: axis along X, small spigot at -X, big socket at +X
R_BIG = 50.0          # outer radius of the socket (big end)
R_SMALL = 37.2        # outer radius of the spigot (small end)
L_TOTAL = 74.85       # overall length along X
L_BIG = 33.45         # length of the big cylindrical socket
CONE_LEN = 3.0        # axial length of the steep outer transition cone
FILLET_OUT = 2.6      # concave fillet where spigot meets the cone

R_BORE_BIG = 42.4     # socket bore radius
R_BORE_SMALL = 34.05  # spigot bore radius
BORE_DEPTH = 30.85    # depth of the socket bore (to the internal shoulder)
FILLET_SH_OUT = 2.8   # concave fillet at socket bore / shoulder
FILLET_SH_IN = 2.4    # round at shoulder / spigot bore

LIP = 0.35            # wall left at the spigot end face (after the inner lead-in)
LEAD_LEN = 8.0        # axial length of the rounded inner lead-in at the spigot end

# angular position of the revolve seams (deg about X, from +Y); placed where they
# graze the silhouette in the standard views
SEAM_OUT = -50.0
SEAM_IN = 130.0

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived positions ----------------
x_small_end = 0.0
x_big_end = L_TOTAL
x_cone_top = L_TOTAL - L_BIG            # start of big cylinder
x_cone_bot = x_cone_top - CONE_LEN      # end of spigot cylinder
x_shoulder = L_TOTAL - BORE_DEPTH       # internal shoulder plane


def round_corner(p_prev, p, p_next, radius):
    """Tangent points and arc mid-point of a fillet of `radius` at corner p of a polyline."""
    ax, ay = p_prev[0] - p[0], p_prev[1] - p[1]
    bx, by = p_next[0] - p[0], p_next[1] - p[1]
    la, lb = math.hypot(ax, ay), math.hypot(bx, by)
    ax, ay, bx, by = ax / la, ay / la, bx / lb, by / lb
    phi = math.acos(max(-1.0, min(1.0, ax * bx + ay * by)))   # corner angle
    t = radius / math.tan(phi / 2.0)                           # tangent distance
    hx, hy = ax + bx, ay + by
    lh = math.hypot(hx, hy)
    hx, hy = hx / lh, hy / lh                                   # bisector
    dc = radius / math.sin(phi / 2.0)                          # corner -> arc centre
    t1 = (p[0] + ax * t, p[1] + ay * t)
    t2 = (p[0] + bx * t, p[1] + by * t)
    mid = (p[0] + hx * (dc - radius), p[1] + hy * (dc - radius))
    return t1, mid, t2


def revolve_profile(pts, radii, seam_angle):
    """Closed (x, r) polyline with rounded corners (radii[i] at pts[i], 0 = sharp),
    revolved 360 deg about the X axis; the seam is turned to seam_angle (deg about X)."""
    n = len(pts)
    wp = None
    for i in range(n):
        p_prev, p, p_next = pts[i - 1], pts[i], pts[(i + 1) % n]
        if radii[i] > 0:
            t1, mid, t2 = round_corner(p_prev, p, p_next, radii[i])
            wp = cq.Workplane("XY").moveTo(*t1) if wp is None else wp.lineTo(*t1)
            wp = wp.threePointArc(mid, t2)
        else:
            wp = cq.Workplane("XY").moveTo(*p) if wp is None else wp.lineTo(*p)
    return (
        wp.close()
        .revolve(360, (0, 0, 0), (1, 0, 0))
        .rotate((0, 0, 0), (1, 0, 0), seam_angle)
    )


# outer body: spigot, concave fillet, steep cone, socket cylinder
outer_pts = [
    (x_small_end, 0.0),
    (x_small_end, R_SMALL),
    (x_cone_bot, R_SMALL),
    (x_cone_top, R_BIG),
    (x_big_end, R_BIG),
    (x_big_end, 0.0),
]
outer_radii = [0, 0, FILLET_OUT, 0, 0, 0]
outer = revolve_profile(outer_pts, outer_radii, SEAM_OUT)

# inner cavity (through bore): rounded lead-in at the spigot end, spigot bore,
# rounded internal shoulder, socket bore
eps = 1.0
d_lead = (R_SMALL - LIP) - R_BORE_SMALL                 # radial size of the lead-in
rho = (LEAD_LEN ** 2 + d_lead ** 2) / (2.0 * d_lead)    # lead-in arc radius (tangent to bore)
cx_l, cr_l = x_small_end + LEAD_LEN, R_BORE_SMALL + rho  # lead-in arc centre
a0 = math.atan2(R_SMALL - LIP - cr_l, x_small_end - cx_l)  # angle of the lip point
a1 = -math.pi / 2.0                                        # angle of the tangent point
am = 0.5 * (a0 + a1)
lead_mid = (cx_l + rho * math.cos(am), cr_l + rho * math.sin(am))

# shoulder corners, rounded in the profile
sh_in = round_corner((x_small_end + LEAD_LEN, R_BORE_SMALL), (x_shoulder, R_BORE_SMALL),
                     (x_shoulder, R_BORE_BIG), FILLET_SH_IN)
sh_out = round_corner((x_shoulder, R_BORE_SMALL), (x_shoulder, R_BORE_BIG),
                      (x_big_end, R_BORE_BIG), FILLET_SH_OUT)

inner = (
    cq.Workplane("XY")
    .moveTo(x_small_end - eps, 0.0)
    .lineTo(x_small_end - eps, R_SMALL - LIP)
    .lineTo(x_small_end, R_SMALL - LIP)
    .threePointArc(lead_mid, (x_small_end + LEAD_LEN, R_BORE_SMALL))
    .lineTo(*sh_in[0])
    .threePointArc(sh_in[1], sh_in[2])
    .lineTo(*sh_out[0])
    .threePointArc(sh_out[1], sh_out[2])
    .lineTo(x_big_end + eps, R_BORE_BIG)
    .lineTo(x_big_end + eps, 0.0)
    .close()
    .revolve(360, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_IN)
)

body = outer.cut(inner)
result = body
